"""Three-key membrane / keypad plate.

A thin parallelogram plate (45 deg slanted ends, rounded corners) standing in
the XZ plane carries three parallelogram keys protruding towards -Y, each with
a rounded front and an engraved symbol (previous / play / next).  Two slanted
slots pierce the plate between the keys.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
SLANT_DEG = 45.0          # slant of the parallelogram ends (from horizontal)

PLATE_W = 95.5            # horizontal width of plate at mid height
PLATE_H = 18.8            # plate height (Z)
PLATE_T = 2.15            # plate thickness (Y)
PLATE_R = 4.8             # plate corner radius (in plan)

BTN_W = 17.4              # horizontal width of a key at mid height
BTN_H = 11.85             # key height (Z)
BTN_D = 6.8               # key protrusion from plate front face (-Y)
BTN_PITCH = 30.0          # key pitch along X
BTN_OFFSET = -4.1         # X offset of the key row from plate centre
BTN_R = 1.5               # key corner radius (in plan)
BTN_ZOFF = 0.0            # vertical offset of the key row from plate centre
BTN_FILLET = 2.2          # fillet on the key front edges

SLOT_W = 7.8              # horizontal width of slot between keys
SLOT_H = 12.6             # slot height
SLOT_R = 1.8              # slot corner radius

SYM_DEPTH = 1.3           # engraved symbol depth
TRI_SIDE = 3.8            # triangle symbol side (before rounding offset)
TRI_R = 1.2               # triangle rounding offset
CIRC_D = 6.0              # circle symbol diameter

SH = 1.0 / math.tan(math.radians(SLANT_DEG))  # x shift per unit of height


def para_pts(cx, cz, w, h):
    """Parallelogram (horizontal top/bottom, slanted ends) in XZ plane coords."""
    s = h * SH
    return [
        (cx - w / 2 - s / 2, cz - h / 2),
        (cx + w / 2 - s / 2, cz - h / 2),
        (cx + w / 2 + s / 2, cz + h / 2),
        (cx - w / 2 + s / 2, cz + h / 2),
    ]


# ---------------- plate ----------------
plate = (
    cq.Workplane("XZ")
    .polyline(para_pts(0, 0, PLATE_W, PLATE_H)).close()
    .extrude(-PLATE_T)            # XZ normal is -Y, so this goes to +Y
    .edges("|Y").fillet(PLATE_R)
)

# slots through the plate, between keys
for i in (-0.5, 0.5):
    cx = BTN_OFFSET + i * BTN_PITCH
    slot = (
        cq.Workplane("XZ").workplane(offset=1.0)
        .polyline(para_pts(cx, 0, SLOT_W, SLOT_H)).close()
        .extrude(-(PLATE_T + 2.0))
        .edges("|Y").fillet(SLOT_R)
    )
    plate = plate.cut(slot)

# ---------------- keys ----------------
result = plate
for i in (-1, 0, 1):
    cx = BTN_OFFSET + i * BTN_PITCH
    key = (
        cq.Workplane("XZ")
        .polyline(para_pts(cx, BTN_ZOFF, BTN_W, BTN_H)).close()
        .extrude(BTN_D)
        .edges("|Y").fillet(BTN_R)
        .faces("<Y").edges().fillet(BTN_FILLET)
    )
    # engraved symbol on the key face
    wp = cq.Workplane("XZ").workplane(offset=BTN_D - SYM_DEPTH)
    if i == 0:
        sym = wp.center(cx, BTN_ZOFF).circle(CIRC_D / 2).extrude(SYM_DEPTH + 1.0)
    else:
        hgt = TRI_SIDE * math.sqrt(3) / 2
        d = -1 if i < 0 else 1     # pointing direction
        pts = [
            (cx + d * hgt * 2 / 3, BTN_ZOFF),
            (cx - d * hgt / 3, BTN_ZOFF + TRI_SIDE / 2),
            (cx - d * hgt / 3, BTN_ZOFF - TRI_SIDE / 2),
        ]
        sym = (
            wp.polyline(pts).close().offset2D(TRI_R, "arc")
            .extrude(SYM_DEPTH + 1.0)
        )
    key = key.cut(sym)
    result = result.union(key)

VIEW = {"azimuth": 45, "elevation": 26}
